import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PITCH = 8.0          # hole pitch along each bar
N_HOLES = 11         # holes per side (incl. the two at the corners)
END_OFFSET = 7.9     # outer edge -> centre of the corner holes
BAR_W = 7.8          # in-plane width of each frame bar
THICK = 7.4          # frame thickness (Y direction)
HOLE_D = 4.8         # pin hole diameter
CBORE_D = 6.3        # counterbore diameter on the outer faces
CBORE_DEPTH = 0.8    # counterbore depth
HOLE_DEPTH = END_OFFSET   # holes end on the plane of the corner-hole axes

HALF_SPAN = (N_HOLES - 1) / 2.0 * PITCH       # centre of outermost holes
OUTER = 2.0 * (HALF_SPAN + END_OFFSET)        # overall outer size
INNER = OUTER - 2.0 * BAR_W                   # opening size
H = OUTER / 2.0

# ---------------- frame body: square ring in the XZ plane ----------------
frame = (
    cq.Workplane("XZ")
    .rect(OUTER, OUTER)
    .extrude(THICK / 2.0, both=True)
)
opening = (
    cq.Workplane("XZ")
    .rect(INNER, INNER)
    .extrude(THICK, both=True)
)
frame = frame.cut(opening)

# ---------------- counterbored cross holes in the four bars ----------------
# one row of N_HOLES holes on every outer edge face, drilled inward across
# the bar width; the end holes sit at the inner corners and cross the end
# hole of the neighbouring bar.
positions = [(-HALF_SPAN + i * PITCH, 0.0) for i in range(N_HOLES)]

# (xDir only orients the cylinder seams; the hole rows are symmetric)
edge_planes = [
    cq.Plane(origin=(0, 0, H), xDir=(-1, 0, 0), normal=(0, 0, 1)),    # top
    cq.Plane(origin=(0, 0, -H), xDir=(-1, 0, 0), normal=(0, 0, -1)),  # bottom
    cq.Plane(origin=(H, 0, 0), xDir=(0, 0, -1), normal=(1, 0, 0)),    # right
    cq.Plane(origin=(-H, 0, 0), xDir=(0, 0, -1), normal=(-1, 0, 0)),  # left
]

for pl in edge_planes:
    frame = (
        frame.copyWorkplane(cq.Workplane(pl))
        .pushPoints(positions)
        .cboreHole(HOLE_D, CBORE_D, CBORE_DEPTH, depth=HOLE_DEPTH)
    )

result = frame

VIEW = {"azimuth": 45, "elevation": 26}
